import math
import cadquery as cq

# ---------------------------------------------------------------
# Card-guide mounting plate.
# Plate lies in the XZ plane, back face at +Y, all features on the
# front (-Y) face.  "Depth" values are measured from the plate front
# face (Y = 0) toward the viewer (-Y).
# ---------------------------------------------------------------

# base plate
W = 100.0          # width  (X)
H = 150.0          # height (Z)
T = 3.3            # thickness
BEVEL = 2.9        # back-edge bevel inset (full-thickness bevel)

# mounting holes (countersunk from the back)
HOLE_D = 3.5
CSK_D = 6.5
HOLE_X = W / 2 - 9.2
HOLE_Z = H / 2 - 9.0

# perimeter rim wall
RIM_A = 43.2       # outer half width
RIM_B = 68.4       # outer half height
RIM_C = 10.5       # corner chamfer
RIM_ND = 6.2       # depth of the V notch around the mid-side holes
RIM_NE = 7.8       # half span of the notch at its base
RIM_W = 2.4        # wall thickness
RIM_H = 3.2        # wall height
RIM_LOW_X = 17.5   # rim lowered to BOX_H between the rails

# raised areas (hollow from the back)
BOX_X = 37.8       # outer half width of the raised square
BOX_Z = 37.7       # half height of the raised square
BOX_H = 2.1        # height above the plate face
STRIP_X0 = 18.5    # raised strips under the rails (card channel floor),
                   # running the full rail length, start at |X| = STRIP_X0
STRIP_H = 2.4      # height of those strips

# back pocket
POCKET_X = 34.0    # half width
POCKET_Z = 34.5    # half height
SHELL = 1.0        # remaining wall thickness under the raised faces
BAR_Z1 = 31.5      # ribs in the pocket along the window top / bottom edges
BAR_X = 31.5
BAR_TOP = 1.0      # rib back face position (Y)

# window
WIN_X = 17.5
WIN_Z = 28.2
WIN_TAB_X = 3.4
WIN_TAB_H = 3.0

# L-shaped card rails
RAIL_OUT = 25.1    # outer face |X|
RAIL_WEB = 2.7     # web thickness
RAIL_IN = 19.1     # flange tip |X|
RAIL_H = 9.0       # total height
RAIL_FL = 2.8      # flange thickness
RAIL_Z = RIM_B - RIM_W - 0.3   # rails stop at the inner face of the rim

# pads with screw holes + slots
PAD_X0 = RAIL_OUT
PAD_X1 = 34.3
PAD_Z0 = 25.1
PAD_Z1 = 34.6
PAD_H = 5.5
PAD_HOLE_D = 2.2
PAD_CB_D = 3.4     # counterbore of the pad holes from the back
SLOT_W = 2.9

# round snap boss
BOSS_X = -33.3
BOSS_Z = 51.8
BOSS_OD = 17.0
BOSS_ID = 12.0
BOSS_H = 4.7
BOSS_HOLE_D = 10.1
FING_W = 3.3       # snap finger width
FING_H = 6.3       # snap finger height
FING_RO = 8.6      # finger outer radius
HOOK = 0.9         # inward hook at the finger tip
HOOK_H = 1.4
FING_CH = 0.8      # chamfer on the outer tip of the finger
SLIT_W = 2.0

# small hexagonal mark on the back
MARK_Z = 63.5
MARK_D = 3.6
MARK_DEPTH = 0.5


def front(depth0=0.0):
    """XZ workplane at the given depth in front of the plate (extrudes toward -Y)."""
    return cq.Workplane("XZ", origin=(0, -depth0, 0))


def box(x0, x1, z0, z1, d0, d1):
    """Axis aligned block: X in [x0,x1], Z in [z0,z1], depth from d0 to d1."""
    return (front(d0).center((x0 + x1) / 2, (z0 + z1) / 2)
            .rect(abs(x1 - x0), abs(z1 - z0)).extrude(d1 - d0))


# ---------------- base plate (bevelled back edges) ----------------
taper = math.degrees(math.atan(BEVEL / T))
part = cq.Workplane("XZ").rect(W, H).extrude(-T, taper=taper)

# ---------------- rim wall ----------------
def rim_outline(a, b, c, nd, ne):
    nf = ne - nd
    return [
        (-a + c, b), (a - c, b), (a, b - c),
        (a, ne), (a - nd, nf), (a - nd, -nf), (a, -ne),
        (a, -b + c), (a - c, -b), (-a + c, -b), (-a, -b + c),
        (-a, -ne), (-a + nd, -nf), (-a + nd, nf), (-a, ne),
        (-a, b - c),
    ]


outer_w = front().polyline(rim_outline(RIM_A, RIM_B, RIM_C, RIM_ND, RIM_NE)).close().wires().val()
inner_w = outer_w.offset2D(-RIM_W, "intersection")[0]
rim_face = cq.Face.makeFromWires(outer_w, [inner_w])
rim = cq.Workplane("XZ").add(cq.Solid.extrudeLinear(rim_face, cq.Vector(0, -RIM_H, 0)))
rim = rim.cut(box(-RIM_LOW_X, RIM_LOW_X, -RIM_B - 1, RIM_B + 1, BOX_H, RIM_H + 1))
part = part.union(rim)

# ---------------- raised areas ----------------
raised = box(-BOX_X, BOX_X, -BOX_Z, BOX_Z, 0, BOX_H)
for s in (-1, 1):
    raised = raised.union(box(s * STRIP_X0, s * RAIL_OUT, -RAIL_Z, RAIL_Z, 0, STRIP_H))
part = part.union(raised)

# ---------------- rails ----------------
for s in (-1, 1):
    pts = [
        (s * RAIL_OUT, 0), (s * RAIL_OUT, RAIL_H), (s * RAIL_IN, RAIL_H),
        (s * RAIL_IN, RAIL_H - RAIL_FL), (s * (RAIL_OUT - RAIL_WEB), RAIL_H - RAIL_FL),
        (s * (RAIL_OUT - RAIL_WEB), 0),
    ]
    rail = (cq.Workplane("XY", origin=(0, 0, -RAIL_Z))
            .polyline([(x, -d) for x, d in pts]).close().extrude(2 * RAIL_Z))
    part = part.union(rail)

# ---------------- pads ----------------
for sx in (-1, 1):
    for sz in (-1, 1):
        part = part.union(box(sx * PAD_X0, sx * PAD_X1, sz * PAD_Z0, sz * PAD_Z1, 0, PAD_H))

# ---------------- snap boss ----------------
boss = (front().center(BOSS_X, BOSS_Z).circle(BOSS_OD / 2)
        .circle(BOSS_ID / 2).extrude(BOSS_H))
for sz in (-1, 1):
    # slits beside each snap finger
    for sx in (-1, 1):
        cx = BOSS_X + sx * (FING_W / 2 + SLIT_W / 2)
        boss = boss.cut(box(cx - SLIT_W / 2, cx + SLIT_W / 2,
                            BOSS_Z + sz * (BOSS_ID / 2 - 1.0), BOSS_Z + sz * (BOSS_OD / 2 + 1.0),
                            1.2, BOSS_H + 1))
    # finger with an inward hook and lead-in chamfer at its tip
    ri = BOSS_ID / 2
    prof = [
        (0.0, ri), (0.0, FING_RO), (-FING_H + FING_CH, FING_RO),
        (-FING_H, FING_RO - FING_CH), (-FING_H, ri - HOOK + 0.5),
        (-FING_H + 0.5, ri - HOOK), (-FING_H + HOOK_H, ri - HOOK),
        (-FING_H + HOOK_H, ri),
    ]
    fing = (cq.Workplane("YZ", origin=(BOSS_X - FING_W / 2, 0, 0))
            .polyline([(y, BOSS_Z + sz * r) for y, r in prof]).close()
            .extrude(FING_W))
    boss = boss.union(fing)
part = part.union(boss)

# ---------------- cuts ----------------
# window with a small tab notch in its top edge
part = part.cut(box(-WIN_X, WIN_X, -WIN_Z, WIN_Z, -T - 1, RAIL_H + 1))
part = part.cut(box(-WIN_TAB_X, WIN_TAB_X, WIN_Z - 1, WIN_Z + WIN_TAB_H, -T - 1, BOX_H + 1))

# back pocket behind the raised square (thin shell), with two ribs
# along the top and bottom edges of the window
pocket = box(-POCKET_X, POCKET_X, -POCKET_Z, POCKET_Z, -T - 1, BOX_H - SHELL)
for sz in (-1, 1):
    pocket = pocket.cut(box(-BAR_X, BAR_X, sz * WIN_Z, sz * BAR_Z1, -BAR_TOP, BOX_H))
part = part.cut(pocket)

# slots between the pads
for sx in (-1, 1):
    part = part.cut(box(sx * PAD_X0, sx * (PAD_X0 + SLOT_W), -PAD_Z0, PAD_Z0,
                        -T - 1, PAD_H + 1))

# pad screw holes
for sx in (-1, 1):
    for sz in (-1, 1):
        cx = sx * (PAD_X0 + PAD_X1) / 2
        cz = sz * (PAD_Z0 + PAD_Z1) / 2
        part = part.cut(front(-T - 1).center(cx, cz).circle(PAD_HOLE_D / 2)
                        .extrude(T + PAD_H + 2))
        part = part.cut(front(-T - 1).center(cx, cz).circle(PAD_CB_D / 2)
                        .extrude(T + 1 + BOX_H - SHELL))

# snap boss through hole
part = part.cut(front(-T - 1).center(BOSS_X, BOSS_Z).circle(BOSS_HOLE_D / 2)
                .extrude(T + 2))

# mounting holes, countersunk from the back
pts = []
for sx in (-1, 1):
    for zz in (-HOLE_Z, 0, HOLE_Z):
        pts.append((sx * HOLE_X, zz))
part = part.cut(front(-T - 1).pushPoints(pts).circle(HOLE_D / 2).extrude(T + 2))
for x, z in pts:
    cone = cq.Solid.makeCone(CSK_D / 2 + 0.5, 0.0, CSK_D / 2 + 0.5,
                             pnt=cq.Vector(x, T + 0.5, z), dir=cq.Vector(0, -1, 0))
    part = part.cut(cq.Workplane().add(cone))

# small hexagonal mark on the back face
part = part.cut(front(-T).center(0, MARK_Z).polygon(6, MARK_D).extrude(MARK_DEPTH))

result = part

VIEW = {"azimuth": 45, "elevation": 26}
